import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
DISC_D = 100.0        # base disc diameter
DISC_T = 3.3          # base disc thickness

HOUSING_R = 22.8      # outer radius of the housing (centred on disc axis)
HOUSING_H = 22.6      # housing height above the disc top
FRONT_Y = -12.4       # most forward point of the front lip arc
CORNER_Y = -7.1       # y where the lip arc meets the outer circle (pillar plane)

BORE_R = 18.0         # inner cavity radius
LIP_Z = 14.3          # underside of the cap / top of the front opening
LIP_CH_V = 2.0        # chamfer on the lip bottom front edge (vertical)
LIP_CH_H = 1.3        # chamfer on the lip bottom front edge (horizontal)

WIN_W = 8.0           # rectangular window through the back wall
WIN_H = 8.3

DHOLE_R = 6.4         # D-shaped hole through the cap
DHOLE_CY = -1.1       # centre of the D circle
DHOLE_FLAT_Y = -4.2   # flat of the D (towards the front)

TOP_FILLET = 1.8      # rounding of the cap top edge
BASE_FILLET = 2.0     # fillet housing -> disc (outside)
EDGE_ROUND = 0.75     # rounding of the vertical inner edges of the two pillars

# ---------------- derived ----------------
corner_x = math.sqrt(HOUSING_R ** 2 - CORNER_Y ** 2)
# front arc through (+-corner_x, CORNER_Y) and (0, FRONT_Y)
sag = CORNER_Y - FRONT_Y
ARC_R = (corner_x ** 2 + sag ** 2) / (2.0 * sag)
ARC_CY = FRONT_Y + ARC_R
BIG = 80.0


def revolve_z(pts_fn, about_y=0.0):
    """Revolve a closed (r, z) profile 360 deg about a vertical axis at (0, about_y)."""
    return pts_fn(cq.Workplane("XZ")).close().revolve(360, (0, 0, 0), (0, 1, 0)).translate((0, about_y, 0))


# ---------------- base disc ----------------
disc = cq.Workplane("XY").circle(DISC_D / 2.0).extrude(-DISC_T)

# ---------------- housing: revolved body with base flare and rounded top ----------------
R, H, fb, ft = HOUSING_R, HOUSING_H, BASE_FILLET, TOP_FILLET
s2 = math.sqrt(0.5)
housing = revolve_z(
    lambda w: w.moveTo(0, 0)
    .lineTo(R + fb, 0)
    .threePointArc((R + fb - fb * s2, fb - fb * s2), (R, fb))
    .lineTo(R, H - ft)
    .threePointArc((R - ft + ft * s2, H - ft + ft * s2), (R - ft, H))
    .lineTo(0, H)
)

# cavity: bore + front opening (everything in front of the pillar plane),
# with the two vertical inner pillar edges rounded
ri, fr = BORE_R, EDGE_ROUND
yc = CORNER_Y + fr                                  # fillet centre y
xc = math.sqrt((ri + fr) ** 2 - yc ** 2)            # fillet centre x
px, py = xc * ri / (ri + fr), yc * ri / (ri + fr)   # tangent point on the bore
sharp_x = math.sqrt(ri ** 2 - CORNER_Y ** 2)        # original sharp corner
dx, dy = sharp_x - xc, CORNER_Y - yc
dl = math.hypot(dx, dy)
mx, my = xc + fr * dx / dl, yc + fr * dy / dl       # a point on the rounding arc
cavity = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .moveTo(-BIG, -BIG)
    .lineTo(BIG, -BIG)
    .lineTo(BIG, CORNER_Y)
    .lineTo(xc, CORNER_Y)
    .threePointArc((mx, my), (px, py))
    .threePointArc((0, ri), (-px, py))
    .threePointArc((-mx, my), (-xc, CORNER_Y))
    .lineTo(-BIG, CORNER_Y)
    .close()
    .extrude(LIP_Z + 1.0)
)
housing = housing.cut(cavity)

# lip: trim the cap with the front arc, rounded at the top
lip_trim = revolve_z(
    lambda w: w.moveTo(ARC_R, LIP_Z - 0.5)
    .lineTo(ARC_R + 30.0, LIP_Z - 0.5)
    .lineTo(ARC_R + 30.0, H + 1.0)
    .lineTo(ARC_R - ft, H + 1.0)
    .lineTo(ARC_R - ft, H)
    .threePointArc((ARC_R - ft + ft * s2, H - ft + ft * s2), (ARC_R, H - ft)),
    about_y=ARC_CY,
)
housing = housing.cut(lip_trim)

# chamfer along the lip bottom front edge (only in front of the pillar plane)
k = LIP_CH_V / LIP_CH_H
ext = 6.0
ring = revolve_z(
    lambda w: w.moveTo(ARC_R - LIP_CH_H, LIP_Z - 0.01)
    .lineTo(ARC_R + ext, LIP_Z - 0.01)
    .lineTo(ARC_R + ext, LIP_Z + (LIP_CH_H + ext) * k),
    about_y=ARC_CY,
)
front_zone = (
    cq.Workplane("XY")
    .box(BIG, BIG, H + 5.0, centered=(True, False, False))
    .translate((0, CORNER_Y - BIG, 0))
)
housing = housing.cut(ring.intersect(front_zone))

# rectangular window at the bottom of the back wall
win = (
    cq.Workplane("XY")
    .box(WIN_W, R, WIN_H + 1.0, centered=(True, False, False))
    .translate((0, BORE_R - 3.0, -1.0))
)
housing = housing.cut(win)

# D-shaped hole through the cap (flat towards the front)
half = math.sqrt(DHOLE_R ** 2 - (DHOLE_FLAT_Y - DHOLE_CY) ** 2)
dhole = (
    cq.Workplane("XY")
    .workplane(offset=LIP_Z - 1.0)
    .moveTo(-half, DHOLE_FLAT_Y)
    .lineTo(half, DHOLE_FLAT_Y)
    .threePointArc((0, DHOLE_CY + DHOLE_R), (-half, DHOLE_FLAT_Y))
    .close()
    .extrude(H)
)
housing = housing.cut(dhole)

result = disc.union(housing)

VIEW = {"azimuth": 45, "elevation": 26}
